import math
import cadquery as cq

# ---------------------------------------------------------------
# Disc-shaped force/torque sensor with cable strain relief.
# Disc axis = X.  Front (tool) face = +X, back (mounting) face = -X.
# Angles of face features are measured in the YZ plane from +Y
# towards +Z.
# ---------------------------------------------------------------

VIEW = {"azimuth": 45, "elevation": 26}

# --- main body --------------------------------------------------
D = 100.0            # outer diameter
R = D / 2.0
T = 38.0             # body thickness (along X)
FRONT_FILLET = 3.0   # round on the front outer edge
XF = T / 2.0         # front face x
XB = -T / 2.0        # back face x

# --- centre through hole ----------------------------------------
CH_D = 16.8
CH_CHAMF = 1.2       # chamfer at the front face

# --- socket head cap screws in counterbores (front face) ---------
SCR_R = 37.35
SCR_ANGLES = [40, 80, 160, 200, 280, 320]
HEX_ROT = [0, 30, 0, 30, 30, 30]   # hex socket orientation (deg)
CB_D = 16.8          # counterbore diameter
HEAD_D = 14.8        # screw head diameter
HEAD_RECESS = 0.5    # head top below front face
CB_DEPTH = 3.0       # depth of annular gap around head
HEX_AF = 6.9         # hex socket across flats
HEX_DEPTH = 4.0

# --- plain blind holes on front face -----------------------------
MH_R = 33.5
MH_ANGLES = [-18, 18, 102, 138, 222, 258]
MH_D = 8.6
MH_DEPTH = 10.0

SA_R = 39.9          # dowel holes (larger)
SA_D = 7.0
SA_ANGLES = [0, 120]
SB_R = 37.3          # dowel holes (smaller)
SB_D = 5.0
SB_ANGLES = [180, 300]
S_DEPTH = 8.0

# --- back boss ----------------------------------------------------
BOSS_R = 29.6
BOSS_H = 1.0
NOTCH_ANGLES = [0, 120, 240]
NOTCH_BOTTOM = 23.0  # radius at the bottom of each notch
NOTCH_W = 14.8       # width of the inner notch slot
NOTCH_FILLET = 3.0   # corner radius of the notch slot
SHELF_R = 26.3       # distance of the flat shelf cut from the centre
BH_R = 22.2
BH_D = 9.4
BH_ANGLES = [40, 80, 160, 200, 280, 320]
BH_DEPTH = 10.0

# --- cable strain relief -----------------------------------------
CABLE_ANG = 60.0     # radial direction in YZ plane (deg from +Y)
CABLE_X = 7.9        # axial (X) position of the cable
BOOT_START = R - 6.0 # distance from disc axis where the boot starts
BOOT_END = 79.6
BOOT_D0 = 8.7        # boot diameter at the body
BOOT_D1 = 7.9        # boot diameter at its outer end
TIP_D = 5.9
TIP_END = 86.9
ENTRY_D = 10.2       # entry counterbore in the rim
ENTRY_DEPTH = 2.5
SLOT_R = 1.2         # strain-relief groove radius
SLOT_LEN = 12.0      # groove cutter length (across the cable)
SLOT_DEPTH = 1.9     # groove depth below boot surface
SLOTS_P = [56.2, 64.3, 72.4]   # slot pairs cut from the +-tangential sides
SLOTS_Q = [60.4, 68.5, 76.6]   # slot pairs cut from the +-X sides


def polar(r, a_deg):
    a = math.radians(a_deg)
    return (r * math.cos(a), r * math.sin(a))


def yz(x0):
    """Workplane parallel to YZ at x = x0 (local x = Y, local y = Z)."""
    return cq.Workplane("YZ").workplane(offset=x0)


# ---------------- body ----------------
body = yz(XB).circle(R).extrude(T)
body = body.faces(">X").edges().fillet(FRONT_FILLET)

# back boss with three stepped notches (flat shelf + rounded slot)
boss = yz(XB - BOSS_H).circle(BOSS_R).extrude(BOSS_H + 0.5)
ROUT = BOSS_R + 5.0
for a in NOTCH_ANGLES:
    slot = (
        yz(XB - BOSS_H - 1)
        .center((NOTCH_BOTTOM + ROUT) / 2, 0)
        .rect(ROUT - NOTCH_BOTTOM, NOTCH_W)
        .extrude(BOSS_H + 1)
        .edges("|X")
        .fillet(NOTCH_FILLET)
    )
    shelf = (
        yz(XB - BOSS_H - 1)
        .center((SHELF_R + ROUT) / 2, 0)
        .rect(ROUT - SHELF_R, 2 * BOSS_R)
        .extrude(BOSS_H + 1)
    )
    cutter = slot.union(shelf).rotate((0, 0, 0), (1, 0, 0), a)
    boss = boss.cut(cutter)
body = body.union(boss)

# centre through hole, chamfered at the front face
body = body.cut(yz(XB - BOSS_H - 2).circle(CH_D / 2).extrude(T + BOSS_H + 4))
cone = cq.Solid.makeCone(
    CH_D / 2 + CH_CHAMF + 0.5, CH_D / 2 - 0.01, CH_CHAMF + 0.5,
    pnt=cq.Vector(XF + 0.5, 0, 0), dir=cq.Vector(-1, 0, 0),
)
body = body.cut(cq.Workplane().add(cone))

# screws: recessed head, narrow annular gap, hex socket
scr_pts = [polar(SCR_R, a) for a in SCR_ANGLES]
body = body.cut(
    yz(XF - HEAD_RECESS).pushPoints(scr_pts).circle(CB_D / 2).extrude(HEAD_RECESS + 1)
)
body = body.cut(
    yz(XF - CB_DEPTH)
    .pushPoints(scr_pts)
    .circle(CB_D / 2)
    .circle(HEAD_D / 2)
    .extrude(CB_DEPTH + 1)
)
hex_d = HEX_AF / math.cos(math.radians(30))  # circumscribed diameter
for (u, v), rot in zip(scr_pts, HEX_ROT):
    sock = (
        yz(XF - HEAD_RECESS - HEX_DEPTH)
        .center(u, v)
        .transformed(rotate=(0, 0, rot))
        .polygon(6, hex_d)
        .extrude(HEX_DEPTH + 1)
    )
    body = body.cut(sock)

# plain blind holes on the front face
for r, angs, d, depth in (
    (MH_R, MH_ANGLES, MH_D, MH_DEPTH),
    (SA_R, SA_ANGLES, SA_D, S_DEPTH),
    (SB_R, SB_ANGLES, SB_D, S_DEPTH),
):
    body = body.cut(
        yz(XF - depth).pushPoints([polar(r, a) for a in angs]).circle(d / 2).extrude(depth + 1)
    )

# blind holes in the back boss
body = body.cut(
    yz(XB - BOSS_H - 1)
    .pushPoints([polar(BH_R, a) for a in BH_ANGLES])
    .circle(BH_D / 2)
    .extrude(BH_DEPTH + 1)
)

# ---------------- cable strain relief ----------------
ca = math.radians(CABLE_ANG)
adir = cq.Vector(0, math.cos(ca), math.sin(ca))      # cable axis (radial)
tdir = cq.Vector(0, -math.sin(ca), math.cos(ca))     # tangential
ndir = cq.Vector(1, 0, 0)                            # disc axis
base = cq.Vector(CABLE_X, 0, 0)


def on_axis(rho):
    return base + adir * rho


def boot_r(rho):
    f = (rho - BOOT_START) / (BOOT_END - BOOT_START)
    return BOOT_D0 / 2 + f * (BOOT_D1 - BOOT_D0) / 2


# entry counterbore in the rim
entry = cq.Solid.makeCylinder(ENTRY_D / 2, 20.0, on_axis(R - ENTRY_DEPTH), adir)
body = body.cut(cq.Workplane().add(entry))

boot = cq.Solid.makeCone(
    BOOT_D0 / 2, BOOT_D1 / 2, BOOT_END - BOOT_START, on_axis(BOOT_START), adir
)
tip = cq.Solid.makeCylinder(
    TIP_D / 2, TIP_END - BOOT_END + 0.5, on_axis(BOOT_END - 0.5), adir
)
cable = cq.Workplane().add(boot).union(cq.Workplane().add(tip))

# strain-relief grooves: opposed pairs of round cross-cuts, alternating
# by 90 degrees along the boot (cutter axes perpendicular to the boot)
def groove_cut(rho, side_dir, axis_dir):
    off = boot_r(rho) + SLOT_R - SLOT_DEPTH
    p0 = on_axis(rho) + side_dir * off - axis_dir * (SLOT_LEN / 2)
    return cq.Workplane().add(cq.Solid.makeCylinder(SLOT_R, SLOT_LEN, p0, axis_dir))


for rho in SLOTS_P:
    for s in (1.0, -1.0):
        cable = cable.cut(groove_cut(rho, tdir * s, ndir))
for rho in SLOTS_Q:
    for s in (1.0, -1.0):
        cable = cable.cut(groove_cut(rho, ndir * s, tdir))

body = body.union(cable)

result = body
